"""RC-car style wheel: treaded tyre on an 8-spoke 'turbine' rim.

Wheel axis = Z, front (hub dish side) = +Z.  The tyre and rim barrel are one
revolved ring; the spoke web is a disc with eight petal-shaped openings
(vertical walls with a one-sided bevel at both faces); the hub carries a
conical dish and five counterbored bolt holes; the tread is a directional
herringbone of narrow grooves repeated 15 times around the circumference.
"""
import math
import cadquery as cq

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- driving dimensions (mm) ----------------
R_TIRE = 32.0          # tread outer radius
Z_SHOULDER = 10.75     # tire side face height at shoulder
Z_BEAD = 10.75         # tire side face height at bead (flat side face)
SHOULDER_FILLET = 2.0
SEAM_ANGLE = 225.0     # revolve seam placed at a silhouette of the main view
R_BEAD = 24.2          # tire inner edge (front)
R_BARREL = 23.1        # rim barrel inner radius
Z_LEDGE = 9.95         # front rim ledge height
WEB_TOP = 7.1          # front face of spoke web
WEB_BOT = -7.0         # back face of spoke web

N_SPOKES = 8

HUB_R = 6.6
HUB_TOP = 7.3          # hub face stands slightly proud of the web
HUB_DISH_R = 6.35
HUB_DISH_DEPTH = 2.8
N_BOLTS = 5
BOLT_PCD_R = 4.0
CBORE_D = 4.0
CBORE_FLOOR = 5.0
BOLT_D = 2.0

# tread
N_PITCH = 15
X_PHASE = 10.3         # deg, angular position of a centre-line crossing

# ---------------- tire + rim barrel (revolved) ----------------
_f = SHOULDER_FILLET
# side face rises slightly toward the bead; shoulder round is tangent to it
_slope = math.atan2(Z_BEAD - Z_SHOULDER, R_TIRE - _f - R_BEAD)
_a_end = math.pi / 2 - _slope
_zc = Z_BEAD - _f * math.sin(_a_end) - math.tan(_slope) * (
    R_TIRE - _f + _f * math.cos(_a_end) - R_BEAD)
_pe = (R_TIRE - _f + _f * math.cos(_a_end), _zc + _f * math.sin(_a_end))
_pm = (R_TIRE - _f + _f * math.cos(_a_end / 2), _zc + _f * math.sin(_a_end / 2))
prof = (
    cq.Workplane("XZ")
    .moveTo(R_BARREL, -Z_BEAD)
    .lineTo(_pe[0], -_pe[1])
    .threePointArc((_pm[0], -_pm[1]), (R_TIRE, -_zc))
    .lineTo(R_TIRE, _zc)
    .threePointArc(_pm, _pe)
    .lineTo(R_BEAD, Z_BEAD)
    .lineTo(R_BEAD, Z_LEDGE)
    .lineTo(R_BARREL, Z_LEDGE)
    .close()
)
tire = prof.revolve(360, (0, 0, 0), (0, 1, 0)).rotate((0, 0, 0), (0, 0, 1), SEAM_ANGLE)

# ---------------- spoke web with petal openings ----------------
web = (cq.Workplane("XY").workplane(offset=WEB_BOT)
       .circle(R_BARREL + 0.4).extrude(WEB_TOP - WEB_BOT))

# petal outline at the front face, petal tip pointing to +Y (12 o'clock).
# CW-side points (x > 0 side) carry a steep one-sided bevel at the faces.
PETAL_CW = [(0.75, 7.55), (1.85, 9.1), (4.21, 10.88), (6.72, 13.22),
            (7.90, 15.76), (7.98, 17.9), (7.17, 20.34), (5.69, 22.17),
            (5.4, 23.7)]
PETAL_END = [(3.7, 24.5)]
PETAL_CCW = [(2.3, 24.0), (1.26, 22.78), (-1.26, 21.26), (-2.87, 18.71),
             (-3.14, 16.17), (-2.87, 13.22), (-2.11, 10.27), (-1.26, 7.73)]
PETAL_TIP = [(-1.25, 6.3), (-0.2, 5.5), (0.9, 6.2)]
BEVEL_W = 0.90         # horizontal width of the bevel on the CW wall
BEVEL_H = 2.0          # vertical height of that bevel


def shifted_cw(pts, d):
    """move CW-side points into the opening (to the left of travel) by d"""
    out = []
    n = len(pts)
    for i, p in enumerate(pts):
        a = pts[max(i - 1, 0)]
        b = pts[min(i + 1, n - 1)]
        tx, ty = b[0] - a[0], b[1] - a[1]
        ln = math.hypot(tx, ty)
        nx, ny = -ty / ln, tx / ln
        f = d
        if i == 0:
            f = 0.6 * d
        out.append((p[0] + f * nx, p[1] + f * ny))
    return out


PETAL_TOP = PETAL_TIP + PETAL_CW + PETAL_END + PETAL_CCW
PETAL_IN = PETAL_TIP + shifted_cw(PETAL_CW, BEVEL_W) + PETAL_END + PETAL_CCW


def rot(p, a_deg):
    a = math.radians(a_deg)
    c, s = math.cos(a), math.sin(a)
    return (p[0] * c - p[1] * s, p[0] * s + p[1] * c)


def petal_wire(pts, z):
    vs = [cq.Vector(p[0], p[1], z) for p in pts]
    return cq.Wire.assembleEdges([cq.Edge.makeSpline(vs, periodic=True)])


cutters = []
for k in range(N_SPOKES):
    a = k * 360.0 / N_SPOKES
    top = [rot(p, a) for p in PETAL_TOP]
    inn = [rot(p, a) for p in PETAL_IN]
    # one ruled loft: vertical through-opening with a one-sided bevel at
    # both the front and the back face
    secs = [petal_wire(top, WEB_BOT - 0.5), petal_wire(top, WEB_BOT),
            petal_wire(inn, WEB_BOT + BEVEL_H), petal_wire(inn, WEB_TOP - BEVEL_H),
            petal_wire(top, WEB_TOP), petal_wire(top, WEB_TOP + 0.5)]
    cutters.append(cq.Solid.makeLoft(secs, True))

web = web.newObject([web.val().cut(*cutters)])

# ---------------- hub ----------------
hub = (cq.Workplane("XY").workplane(offset=WEB_BOT)
       .circle(HUB_R).extrude(HUB_TOP - WEB_BOT))
web_hub = web.union(hub)

dish = (cq.Workplane("XZ")
        .polyline([(0, HUB_TOP - HUB_DISH_DEPTH), (HUB_DISH_R, HUB_TOP),
                   (HUB_DISH_R, HUB_TOP + 1), (0, HUB_TOP + 1)]).close()
        .revolve(360, (0, 0, 0), (0, 1, 0)))
web_hub = web_hub.cut(dish)

bolt_pts = [(BOLT_PCD_R * math.cos(math.radians(90 + i * 360.0 / N_BOLTS)),
             BOLT_PCD_R * math.sin(math.radians(90 + i * 360.0 / N_BOLTS)))
            for i in range(N_BOLTS)]
cbores = (cq.Workplane("XY").workplane(offset=CBORE_FLOOR)
          .pushPoints(bolt_pts).circle(CBORE_D / 2).extrude(HUB_TOP + 2 - CBORE_FLOOR))
holes = (cq.Workplane("XY").workplane(offset=WEB_BOT - 1)
         .pushPoints(bolt_pts).circle(BOLT_D / 2).extrude(HUB_TOP - WEB_BOT + 3))
web_hub = web_hub.cut(cbores).cut(holes)

# ---------------- tread grooves ----------------
# groove centre line in unrolled coords (s along circumference, z axial),
# relative to a centre-line crossing point.  Each pitch has an S-curve
# running from one shoulder across the centre line to a V apex, plus a
# short return arm; the mirror image (z -> -z) completes the pattern.
G_CURVE = [(-11.0, 11.2), (-10.2, 9.80), (-8.9, 7.73), (-7.7, 6.11),
           (-6.3, 4.36), (-4.85, 2.83), (-2.4, 1.3), (0.0, 0.0),
           (3.12, -1.75), (8.0, -3.0), (12.9, -3.85)]
G_ARM = [(12.9, -3.85), (10.0, -7.75)]
GROOVE_W = 0.7
GROOVE_DEPTH = 0.9


# polyline groups cut from one tangent plane each (indices into the groove
# polyline = G_CURVE + arm end); neighbouring groups share an end point.
G_GROUPS = [(0, 4), (4, 7), (7, 9), (9, 11)]


def groove_tool(th0, pts):
    """cut tool for a run of groove points (unrolled coords), projected onto
    the plane through the run's end points at groove depth"""
    ths = [th0 + p[0] / R_TIRE for p in pts]
    ta, tb = min(ths), max(ths)
    th = 0.5 * (ta + tb)
    half = 0.5 * (tb - ta)
    rfl = R_TIRE - GROOVE_DEPTH
    rin = rfl * math.cos(half)
    origin = cq.Vector(rin * math.cos(th), rin * math.sin(th), 0)
    xdir = cq.Vector(-math.sin(th), math.cos(th), 0)
    normal = cq.Vector(math.cos(th), math.sin(th), 0)
    pl = cq.Plane(origin, xdir, normal)
    loc = [pl.toWorldCoords((rfl * math.sin(t - th), p[1])) for t, p in zip(ths, pts)]
    wire = cq.Wire.makePolygon(loc, close=False)
    outline = wire.offset2D(GROOVE_W / 2, "arc")[0]
    face = cq.Face.makeFromWires(outline)
    return cq.Solid.extrudeLinear(face, normal * (R_TIRE - rin + 1.0))


tools = []
for k in range(N_PITCH):
    th0 = math.radians(X_PHASE + k * 360.0 / N_PITCH)
    for m in (1, -1):
        pts = [(p[0], m * p[1]) for p in G_CURVE + G_ARM[1:]]
        for i0, i1 in G_GROUPS:
            tools.append(groove_tool(th0, pts[i0:i1 + 1]))

tire_cut = tire.val().cut(*tools)

wheel = web_hub.union(cq.Workplane("XY").add(tire_cut))

result = wheel
